import cadquery as cq

# =====================================================================
#  Clip-on cover plate "Domochip WPalaControl V2.0"
#  Plate in the XZ plane (front face at Y=0, facing -Y, engraved text),
#  two guide rails + a trapezoid locating tab on the back (+Y side),
#  open rectangular slot at the bottom edge.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
W = 50.0            # plate width  (X)
H = 57.2            # plate height (Z)
T = 2.0             # plate thickness (Y)
R_CORNER = 5.6      # plate corner radius (all four outer corners)

SLOT_W = 19.7       # open slot at the bottom edge
SLOT_D = 23.5

RAIL_W = 5.3        # rail cross-section across the plate (X)
RAIL_H = 5.3        # rail height above the back face (Y)
RAIL_R = 2.1        # rounded outer/back corner of the rail
RAIL_END = 7.8      # distance from plate top/bottom edge to rail end
PIN_D = 3.8         # small locating pin at each rail end
PIN_L = 0.9
PIN_FILLET = 0.3    # rounded pin tip

TAB_B = 19.6        # trapezoid tab: base width (at the plate)
TAB_T = 13.7        # top width
TAB_H = 2.9         # height above back face (Y)
TAB_Z0 = 3.6        # distance from plate top to tab top
TAB_L = 3.3         # tab size along Z
TAB_X = 0.75        # tab is slightly off-centre towards +X

TXT_DEPTH = 0.6     # engraving depth
TXT_FONT = "DejaVu Sans"
TXT_KIND = "bold"
LINES = [  # text, font size, horizontal squeeze, centre distance below plate top
    ("V2.0", 8.2, 0.855, 7.45),
    ("WPalaControl", 6.86, 0.855, 18.1),
    ("Domochip", 6.86, 0.865, 27.1),
]

# ---------------- plate ----------------
plate = (
    cq.Workplane("XZ")
    .rect(W, H)
    .extrude(-T)                      # XZ normal is -Y, so -T grows towards +Y
    .edges("|Y")
    .fillet(R_CORNER)
)

# open slot from the bottom edge
slot = (
    cq.Workplane("XY")
    .box(SLOT_W, T * 4, SLOT_D + 1.0, centered=(True, True, False))
    .translate((0, T / 2, -H / 2 - 1.0))
)
plate = plate.cut(slot)

# ---------------- guide rails on the back ----------------
rail_len = H - 2 * RAIL_END


def make_rail(sx):
    """Rail along Z at the plate side edge sx=+1 (+X) or sx=-1 (-X)."""
    x_in = sx * (W / 2 - RAIL_W)
    x0 = min(sx * W / 2, x_in)
    r = (
        cq.Workplane("XY")
        .box(RAIL_W, RAIL_H, rail_len, centered=(False, False, True))
        .translate((x0, T, 0))
    )
    # round the outer / back longitudinal edge
    r = (
        r.edges("|Z")
        .edges(">Y")
        .edges(">X" if sx > 0 else "<X")
        .fillet(RAIL_R)
    )
    cx = sx * (W / 2 - RAIL_W / 2)
    cy = T + RAIL_H / 2
    pin_top = (
        cq.Workplane("XY", origin=(cx, cy, rail_len / 2))
        .circle(PIN_D / 2)
        .extrude(PIN_L)
        .faces(">Z").edges()
        .fillet(PIN_FILLET)
    )
    pin_bot = (
        cq.Workplane("XY", origin=(cx, cy, -rail_len / 2))
        .circle(PIN_D / 2)
        .extrude(-PIN_L)
        .faces("<Z").edges()
        .fillet(PIN_FILLET)
    )
    return r.union(pin_top).union(pin_bot)


part = plate.union(make_rail(1)).union(make_rail(-1))

# ---------------- trapezoid locating tab on the back ----------------
tab_ztop = H / 2 - TAB_Z0
tab = (
    cq.Workplane("XY", origin=(TAB_X, 0, tab_ztop - TAB_L))
    .polyline([
        (-TAB_B / 2, T - 0.01),
        (TAB_B / 2, T - 0.01),
        (TAB_T / 2, T + TAB_H),
        (-TAB_T / 2, T + TAB_H),
    ])
    .close()
    .extrude(TAB_L)
)
part = part.union(tab)


# ---------------- engraved text on the front face ----------------
# Text reads upside down (rotated 180 deg) when the front face is viewed.
def engraved_line(txt, fs, sx, zc):
    letters = (
        cq.Workplane("XY")
        .text(txt, fs, -TXT_DEPTH, combine=False, font=TXT_FONT, kind=TXT_KIND,
              halign="center", valign="center")
        .val()
    )
    # slightly condensed lettering
    letters = letters.transformGeometry(
        cq.Matrix([[sx, 0, 0, 0], [0, 1, 0, 0], [0, 0, 1, 0], [0, 0, 0, 1]]))
    bb = letters.BoundingBox()
    letters = letters.translate((-(bb.xmin + bb.xmax) / 2, -(bb.ymin + bb.ymax) / 2, 0))
    # local x -> -X, local y -> -Z, local z -> -Y  (cuts from Y=0 into the plate)
    letters = letters.rotate((0, 0, 0), (1, 0, 0), -90).rotate((0, 0, 0), (0, 0, 1), 180)
    return letters.translate((0, 0, H / 2 - zc))


for txt, fs, sx, zc in LINES:
    try:
        part = part.cut(engraved_line(txt, fs, sx, zc))
    except Exception:
        pass  # lettering is cosmetic; keep the solid if a font is unavailable

result = part
